import math
import cadquery as cq
from OCP.BRepFilletAPI import BRepFilletAPI_MakeFillet

# =====================================================================
#  Flanged elbow housing: round mounting flange, tubular neck with an
#  oblique opening, and a tilted cylindrical gear housing with a bolted
#  round cover.  Flange front face lies in the XZ plane (Y = 0); the
#  body extends towards +Y.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
R_DISK = 100.0      # flange disk radius
T_DISK = 5.0        # flange thickness (front face at Y=0, body towards +Y)
R_TUBE = 55.5       # tube outer radius (axis = Y axis)
R_BORE = 45.0       # bore radius
BORE_START = 15.0   # bore bottom (Y)
BORE_Z = 5.0        # bore axis offset above the tube axis

TILT = 23.0         # housing axis tilt above +X (deg)
PUCK_R = 52.0       # housing radius
PUCK_T = 43.0       # housing thickness
PUCK_Y = 105.9      # housing centre Y
PUCK_V = -95.5      # housing centre in tilted in-plane "up" coordinate
FACE_A = 26.7       # offset of housing outer face plane from tube axis
SLAB_TOP = 40.0     # web top at the flange (in-plane v)
SLAB_BOT = -93.0    # web bottom at the flange (in-plane v)
WEB_FILLET = 16.0   # blend between tube and web side face
UNDER_FILLET = 6.0  # rounding of the web's lower front edge
RIM_FILLET = 6.0    # rounding of the housing face rim

CUT1_N = (-0.362, 0.784, 0.504)  # oblique opening plane normal
CUT1_Y0 = 84.0                   # opening plane crosses tube axis at this Y
CUT2_N = (0.0, 0.746, 0.666)     # upper back chamfer plane normal
CUT2_Y0 = 92.2

# flange front recess (sector)
REC_A0, REC_A1 = 103.0, 127.0    # angular range (deg, from +X towards +Z)
REC_R0 = 60.0
REC_DEPTH = 1.5

# flange back: concave cove web between flange and tube
COVE_A0, COVE_A1 = 128.0, 221.0
COVE_R = 88.0       # outer radius of the cove on the flange
COVE_H = 15.0       # height of the cove on the tube
BEAD_R = 12.0                # quarter-round bead around the tube root ...
BEAD_A0, BEAD_A1 = 100.0, 130.0   # ... over this angular range
BACK_POCKETS = [(0.0, 20.0), (104.0, 124.0), (221.0, 241.0)]  # shallow sector pockets on flange back
BACK_POCKET_DEPTH = 1.5

# housing cover and fasteners
COVER_DV = 3.0      # cover/bolt pattern sits slightly above the housing axis
COVER_R = 35.0
COVER_T = 2.0
BOLT_PCD_R = 40.0
BOLT_PITCH = 20.0
BOLT_ANGLES = [-160.0 + BOLT_PITCH * i for i in range(9)] + [70.0, 90.0, 110.0, 130.0]
BOLT_R = 2.3
BOLT_H = 2.2
SEG_R0, SEG_R1 = 36.5, 47.5      # raised clamp segments radii
SEGMENTS = [(27.0, 60.0, 6.0), (62.0, 144.0, 3.5), (146.0, 182.0, 6.0)]
TAB_ANG = 5.0
TAB_W, TAB_R0, TAB_R1, TAB_H = 7.0, 49.0, 57.0, 8.0

# ribs on the housing side face: (u0, v0, u1, v1)
BARS = [(37.0, -53.0, 57.0, -71.0), (19.0, -71.0, 40.0, -91.0)]
BAR_W, BAR_H = 7.0, 10.0

# block on the housing back face
BOX_U = (72.0, 124.0)
BOX_V = (-126.0, -72.0)
BOX_T = 10.0

th = math.radians(TILT)
n = cq.Vector(math.cos(th), 0, math.sin(th))
ev = cq.Vector(-math.sin(th), 0, math.cos(th))
ey = cq.Vector(0, 1, 0)
SLAB_BACK = FACE_A - PUCK_T


def tilted_plane(a):
    """plane parallel to the housing face, local x = +Y, local y = tilted up"""
    return cq.Plane(origin=n * a, xDir=ey, normal=n)


def tangent_points(p, c, r):
    dx, dy = p[0] - c[0], p[1] - c[1]
    d = math.hypot(dx, dy)
    a = math.acos(r / d)
    b = math.atan2(dy, dx)
    return [(c[0] + r * math.cos(b + s * a), c[1] + r * math.sin(b + s * a)) for s in (1, -1)]


def arc_mid(c, r, p1, p2, ccw):
    a1 = math.atan2(p1[1] - c[1], p1[0] - c[0])
    a2 = math.atan2(p2[1] - c[1], p2[0] - c[0])
    if ccw:
        while a2 <= a1:
            a2 += 2 * math.pi
    else:
        while a2 >= a1:
            a2 -= 2 * math.pi
    am = 0.5 * (a1 + a2)
    return (c[0] + r * math.cos(am), c[1] + r * math.sin(am))


def polar(c, r, ang_deg):
    a = math.radians(ang_deg)
    return (c[0] + r * math.cos(a), c[1] + r * math.sin(a))


def annular_sector(wp, c, r0, r1, a0, a1):
    """closed annular-sector wire on workplane wp (angles in degrees)"""
    am = 0.5 * (a0 + a1)
    return (wp.moveTo(*polar(c, r0, a0)).lineTo(*polar(c, r1, a0))
            .threePointArc(polar(c, r1, am), polar(c, r1, a1))
            .lineTo(*polar(c, r0, a1))
            .threePointArc(polar(c, r0, am), polar(c, r0, a0)).close())


def half_space(normal, y0, big=600):
    m = cq.Vector(*normal).normalized()
    p0 = cq.Vector(0, y0, 0)
    xd = m.cross(cq.Vector(0, 0, 1))
    if xd.Length < 1e-6:
        xd = cq.Vector(1, 0, 0)
    return (cq.Workplane(cq.Plane(origin=p0, xDir=xd.normalized(), normal=m))
            .rect(big, big).extrude(big))


# ---------------- flange disk ----------------
disk = cq.Workplane("XZ").circle(R_DISK).extrude(-T_DISK)  # towards +Y

# shallow sector recess on the flange front face
recess = annular_sector(cq.Workplane("XZ"), (0, 0), REC_R0, R_DISK + 2,
                        REC_A0, REC_A1).extrude(-REC_DEPTH)
disk = disk.cut(recess)

# shallow sector pockets on the flange back face
for p0a, p1a in BACK_POCKETS:
    pocket = annular_sector(cq.Workplane("XZ").workplane(offset=-T_DISK),
                            (0, 0), R_TUBE + 6.0, R_DISK - 3.0,
                            p0a, p1a).extrude(BACK_POCKET_DEPTH)
    disk = disk.cut(pocket)

# ---------------- tube ----------------
BODY_Y0 = T_DISK - 2.0   # web/tube start buried in the flange
tube = (cq.Workplane("XZ").workplane(offset=-BODY_Y0)
        .circle(R_TUBE).extrude(-200))

# ---------------- web joining tube and housing ----------------
C = (PUCK_Y, PUCK_V)
A_top = (BODY_Y0, SLAB_TOP)
A_bot = (BODY_Y0, SLAB_BOT)
T_top = max(tangent_points(A_top, C, PUCK_R), key=lambda q: q[1])
T_bot = min(tangent_points(A_bot, C, PUCK_R), key=lambda q: q[1])
mid_puck = arc_mid(C, PUCK_R, T_top, T_bot, ccw=False)

slab = (cq.Workplane(tilted_plane(SLAB_BACK))
        .moveTo(*A_bot).lineTo(*A_top).lineTo(*T_top)
        .threePointArc(mid_puck, T_bot)
        .close().extrude(PUCK_T))

body = tube.union(slab)

# blend the tube into the flat side face of the web (straight intersection line)
# and slightly round the web's lower front edge
_a = FACE_A
_v = -math.sqrt(R_TUBE ** 2 - _a * _a)
_p = n * _a + ev * _v
_q0 = n * FACE_A + ey * A_bot[0] + ev * A_bot[1]
_q1 = n * FACE_A + ey * T_bot[0] + ev * T_bot[1]
_qm = (_q0 + _q1) * 0.5
_e_blend = body.edges(cq.selectors.BoxSelector((_p.x - 1, 10, _p.z - 1),
                                               (_p.x + 1, 100, _p.z + 1))).vals()
_e_under = body.edges(cq.selectors.BoxSelector((_qm.x - 1, _qm.y - 1, _qm.z - 1),
                                               (_qm.x + 1, _qm.y + 1, _qm.z + 1))).vals()


def _fillet_pairs(shape, pairs):
    mk = BRepFilletAPI_MakeFillet(shape.wrapped)
    for r, edges in pairs:
        for e in edges:
            mk.Add(r, e.wrapped)
    mk.Build()
    return cq.Shape.cast(mk.Shape())


for _r1, _r2 in ((WEB_FILLET, UNDER_FILLET), (10.0, 8.0), (12.0, 6.0), (10.0, 5.0)):
    try:
        _res = _fillet_pairs(body.val(), [(_r1, _e_blend), (_r2, _e_under)])
        if _res.isValid():
            body = cq.Workplane("XY").newObject([_res])
            break
    except Exception:
        pass

# oblique opening and upper chamfer
body = body.cut(half_space(CUT1_N, CUT1_Y0)).cut(half_space(CUT2_N, CUT2_Y0))

# housing puck (not trimmed by the opening planes)
puck = (cq.Workplane(tilted_plane(SLAB_BACK))
        .center(PUCK_Y, PUCK_V).circle(PUCK_R).extrude(PUCK_T))
_rim = [e for e in puck.edges().vals() if abs(e.Center().dot(n) - FACE_A) < 0.01]
puck = puck.newObject(_rim).fillet(RIM_FILLET)
body = body.union(puck)

# block on the housing back face
box = (cq.Workplane(tilted_plane(SLAB_BACK))
       .center(0.5 * (BOX_U[0] + BOX_U[1]), 0.5 * (BOX_V[0] + BOX_V[1]))
       .rect(BOX_U[1] - BOX_U[0], BOX_V[1] - BOX_V[0]).extrude(-BOX_T))
body = body.union(box)

# concave cove web on the flange back
cove_prof = (cq.Workplane("XY")
             .moveTo(R_TUBE - 1, T_DISK - 0.5)
             .lineTo(COVE_R, T_DISK - 0.5)
             .lineTo(COVE_R, T_DISK)
             .threePointArc((R_TUBE + 0.42 * (COVE_R - R_TUBE), T_DISK + 0.30 * COVE_H),
                            (R_TUBE - 1, T_DISK + COVE_H))
             .close()
             .revolve(360, (0, 0, 0), (0, 1, 0)))
am = 0.5 * (COVE_A0 + COVE_A1)
wedge = (cq.Workplane("XZ").moveTo(0, 0)
         .lineTo(*polar((0, 0), 150, COVE_A0))
         .lineTo(*polar((0, 0), 150, am))
         .lineTo(*polar((0, 0), 150, COVE_A1))
         .close().extrude(-60))
cove = cove_prof.intersect(wedge)
body = body.union(cove)

# quarter-round bead at the tube root above the cove
bead = (cq.Workplane("XY")
        .moveTo(R_TUBE - 1, T_DISK - 0.5)
        .lineTo(R_TUBE + BEAD_R, T_DISK - 0.5)
        .lineTo(R_TUBE + BEAD_R, T_DISK)
        .threePointArc((R_TUBE + BEAD_R * math.cos(math.radians(45)),
                        T_DISK + BEAD_R * math.sin(math.radians(45))),
                       (R_TUBE, T_DISK + BEAD_R))
        .lineTo(R_TUBE - 1, T_DISK + BEAD_R)
        .close()
        .revolve(360, (0, 0, 0), (0, 1, 0)))
bm = 0.5 * (BEAD_A0 + BEAD_A1)
bead_wedge = (cq.Workplane("XZ").moveTo(0, 0)
              .lineTo(*polar((0, 0), 150, BEAD_A0))
              .lineTo(*polar((0, 0), 150, bm))
              .lineTo(*polar((0, 0), 150, BEAD_A1))
              .close().extrude(-60))
body = body.union(bead.intersect(bead_wedge))

# bore
bore = (cq.Workplane("XZ").workplane(offset=-BORE_START)
        .center(0, BORE_Z).circle(R_BORE).extrude(-300))
body = body.cut(bore)

# ---------------- housing face details ----------------
face = tilted_plane(FACE_A)
C = (PUCK_Y, PUCK_V + COVER_DV)   # centre of cover, bolts and clamp segments

cover = cq.Workplane(face).center(*C).circle(COVER_R).extrude(COVER_T)
body = body.union(cover)

seg_top = {}
for a0, a1, h in SEGMENTS:
    seg = annular_sector(cq.Workplane(tilted_plane(FACE_A - 3.0)), C, SEG_R0, SEG_R1,
                         a0, a1).extrude(h + 3.0)
    body = body.union(seg)
    seg_top[(a0, a1)] = h

for ang in BOLT_ANGLES:
    base = 0.0
    for (a0, a1), h in seg_top.items():
        if a0 <= ang <= a1:
            base = h
    p = polar(C, BOLT_PCD_R, ang)
    bolt = (cq.Workplane(tilted_plane(FACE_A + base - 0.5)).center(*p)
            .circle(BOLT_R).extrude(BOLT_H + 0.5))
    sock = (cq.Workplane(tilted_plane(FACE_A + base + BOLT_H - 1.0)).center(*p)
            .polygon(6, BOLT_R * 1.1).extrude(2.0))
    body = body.union(bolt.cut(sock))

# radial tab on the housing rim
tab_c = polar(C, 0.5 * (TAB_R0 + TAB_R1), TAB_ANG)
tab = (cq.Workplane(tilted_plane(FACE_A - 2.0)).center(*tab_c)
       .transformed(rotate=(0, 0, TAB_ANG))
       .rect(TAB_R1 - TAB_R0, TAB_W).extrude(TAB_H + 2.0))
body = body.union(tab)

# raised ribs on the side face
for (u0, v0, u1, v1) in BARS:
    L = math.hypot(u1 - u0, v1 - v0)
    ang = math.degrees(math.atan2(v1 - v0, u1 - u0))
    bar = (cq.Workplane(tilted_plane(FACE_A - 3)).center(0.5 * (u0 + u1), 0.5 * (v0 + v1))
           .transformed(rotate=(0, 0, ang))
           .slot2D(L + BAR_W, BAR_W).extrude(BAR_H + 3))
    body = body.union(bar)

result = disk.union(body)
